import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 100.0          # overall length (X)
W = 62.4           # overall width (Y)
H = 7.2            # overall height (Z)
T_WALL = 1.1       # wall thickness (back / left / right)
T_FRONT = 1.4      # front wall thickness
T_FLOOR = 1.25     # floor plate thickness
R_OUT = 3.0        # outer vertical corner radius
R_IN = 1.9         # inner vertical corner radius
BEAD_P = 0.5       # snap bead: inward protrusion (= 45 deg lead-in height)
BEAD_H = 0.3       # snap bead: vertical land below the lead-in
BEAD_BACK_X0, BEAD_BACK_X1 = -40.0, 40.2
BEAD_SIDE_Y = 26.8

# wall vent slots (both long walls)
N_SLOTS = 15
SLOT_PITCH = 5.9
SLOT_W = 1.15
SLOT_LEN = 4.0
SLOT_ZC = 3.7
SLOT_R = 0.3
CH_W, CH_D, CH_TOP = 1.3, 0.3, 0.6   # channels on the front wall inner face

# corner bosses
BOSS_XL, BOSS_XR = -40.5, 42.0
BOSS_YF, BOSS_YB = -25.9, 23.1
BOSS_D = 5.4
BOSS_HOLE = 3.6
BOSS_TOP = 3.5
BOSS_CSK = 0.3

# front wall notch
NOTCH_X0, NOTCH_X1 = -39.7, -36.4
NOTCH_DEPTH = 1.8

# countersunk obround slots
OB_W, OB_LEN = 2.2, 7.6
OB_CSK = 0.9
OB_LEFT = (-23.05, 1.75)
OB_RIGHT = (35.0, 1.9)


def rounded_poly(pts, radii):
    """closed polygon with a fillet radius per vertex -> (start, mid, end) of each corner"""
    n = len(pts)
    out = []
    for i in range(n):
        p0, p1, p2 = pts[i - 1], pts[i], pts[(i + 1) % n]
        r = radii[i]
        d1 = (p1[0] - p0[0], p1[1] - p0[1])
        l1 = math.hypot(*d1)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (p2[0] - p1[0], p2[1] - p1[1])
        l2 = math.hypot(*d2)
        d2 = (d2[0] / l2, d2[1] / l2)
        if r <= 0:
            out.append((p1, None, p1))
            continue
        cosang = -(d1[0] * d2[0] + d1[1] * d2[1])
        theta = math.acos(max(-1.0, min(1.0, cosang)))
        tl = r / math.tan(theta / 2.0)
        a = (p1[0] - d1[0] * tl, p1[1] - d1[1] * tl)
        b = (p1[0] + d2[0] * tl, p1[1] + d2[1] * tl)
        bis = (-d1[0] + d2[0], -d1[1] + d2[1])
        bl = math.hypot(*bis)
        bis = (bis[0] / bl, bis[1] / bl)
        k = r / math.sin(theta / 2.0) - r
        out.append((a, (p1[0] + bis[0] * k, p1[1] + bis[1] * k), b))
    return out


def poly_solid(pts, radii, z0, height):
    tg = rounded_poly(pts, radii)
    wp = cq.Workplane("XY", origin=(0, 0, z0)).moveTo(*tg[0][2])
    n = len(tg)
    for i in range(1, n + 1):
        a, m, b = tg[i % n]
        wp = wp.lineTo(*a)
        if m is not None:
            wp = wp.threePointArc(m, b)
    return wp.close().extrude(height)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY", origin=((x0 + x1) / 2, (y0 + y1) / 2, z0))
            .rect(x1 - x0, y1 - y0).extrude(z1 - z0))


# ---------------- base tray ----------------
outer = (cq.Workplane("XY").rect(L, W).extrude(H)
         .edges("|Z").fillet(R_OUT))
inner = (cq.Workplane("XY", origin=(0, (T_FRONT - T_WALL) / 2, T_FLOOR))
         .rect(L - 2 * T_WALL, W - T_WALL - T_FRONT).extrude(H)
         .edges("|Z").fillet(R_IN))
body = outer.cut(inner)

# snap bead with lead-in chamfer along the inner top edge (left, back and right walls)
p, hb = BEAD_P, BEAD_H
xi, yi = L / 2 - T_WALL, W / 2 - T_WALL
bead_back = (cq.Workplane("YZ", origin=(BEAD_BACK_X0, 0, 0))
             .polyline([(yi + 0.05, H), (yi - p, H - p), (yi - p, H - p - hb), (yi + 0.05, H - p - hb)])
             .close().extrude(BEAD_BACK_X1 - BEAD_BACK_X0))
bead_left = (cq.Workplane("XZ", origin=(0, BEAD_SIDE_Y, 0))
             .polyline([(-xi - 0.05, H), (-xi + p, H - p), (-xi + p, H - p - hb), (-xi - 0.05, H - p - hb)])
             .close().extrude(2 * BEAD_SIDE_Y))
bead_right = (cq.Workplane("XZ", origin=(0, BEAD_SIDE_Y, 0))
              .polyline([(xi + 0.05, H), (xi - p, H - p), (xi - p, H - p - hb), (xi + 0.05, H - p - hb)])
              .close().extrude(2 * BEAD_SIDE_Y))
body = body.union(bead_back).union(bead_left).union(bead_right)

# ---------------- big central cut-out ----------------
cut_pts = [
    (-18.2, 17.7),   # top-left
    (-11.2, 17.7),   # notch bottom-left (concave)
    (-11.2, 26.3),   # notch top-left
    (4.7, 26.3),     # notch top-right
    (4.7, 17.7),     # notch bottom-right (concave)
    (30.1, 17.7),    # top-right
    (30.1, -4.5),    # tab corner (concave of cut-out)
    (36.7, -4.5),
    (36.7, -14.4),
    (20.9, -14.4),   # S step top
    (20.9, -24.0),   # S step bottom
    (-23.2, -24.0),  # lobe bottom-left
    (-23.2, -14.2),  # lobe top-left
    (-18.2, -14.2),  # lobe inner corner (concave)
]
cut_r = [0.4, 1.4, 2.0, 2.2, 2.0, 0.4, 4.4, 0.4, 0.4, 4.0, 4.0, 4.5, 4.5, 0.6]
cutout = poly_solid(cut_pts, cut_r, -1.0, H + 2)
cutout = cutout.union(cq.Workplane("XY", origin=(-18.2, 7.1, -1.0)).circle(2.75).extrude(H + 2))
body = body.cut(cutout)

# ---------------- rectangular floor openings ----------------
rects = [
    (-48.4, -35.3, -6.2, 1.9),                    # A (next to the left wall)
    (-44.6, -32.5, -20.4, -14.0),                 # B
    (37.6, 45.9, -1.9, 9.8),                      # C
    (39.5, 45.9, -19.6, -4.6),                    # D
]
for x0, x1, y0, y1 in rects:
    body = body.cut(box(x0, x1, y0, y1, -1, T_FLOOR + 1))

# ---------------- corner bosses ----------------
boss_pts = [(BOSS_XL, BOSS_YF), (BOSS_XL, BOSS_YB), (BOSS_XR, BOSS_YF), (BOSS_XR, BOSS_YB)]
bosses = (cq.Workplane("XY", origin=(0, 0, T_FLOOR - 0.1)).pushPoints(boss_pts)
          .circle(BOSS_D / 2).extrude(BOSS_TOP - T_FLOOR + 0.1))
body = body.union(bosses)
body = body.cut(cq.Workplane("XY", origin=(0, 0, -1)).pushPoints(boss_pts)
                .circle(BOSS_HOLE / 2).extrude(H + 2))
for bx, by in boss_pts:
    cone = cq.Solid.makeCone(BOSS_HOLE / 2, BOSS_HOLE / 2 + BOSS_CSK + 0.01, BOSS_CSK + 0.01,
                             cq.Vector(bx, by, BOSS_TOP - BOSS_CSK), cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane("XY").add(cone))
    cone_b = cq.Solid.makeCone(BOSS_HOLE / 2 + BOSS_CSK + 0.01, BOSS_HOLE / 2, BOSS_CSK + 0.01,
                               cq.Vector(bx, by, -0.01), cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane("XY").add(cone_b))

# ---------------- countersunk obround slots ----------------
for cx, cy in (OB_LEFT, OB_RIGHT):
    slot = (cq.Workplane("XY", origin=(cx, cy, -1)).slot2D(OB_LEN, OB_W, 90)
            .extrude(T_FLOOR + 2))
    csk = (cq.Workplane("XY", origin=(cx, cy, T_FLOOR - OB_CSK))
           .slot2D(OB_LEN, OB_W, 90)
           .workplane(offset=OB_CSK + 0.01)
           .slot2D(OB_LEN + 2 * OB_CSK, OB_W + 2 * OB_CSK, 90)
           .loft())
    body = body.cut(slot).cut(csk)

# ---------------- vent slots in the long walls ----------------
xs = [(i - (N_SLOTS - 1) / 2.0) * SLOT_PITCH for i in range(N_SLOTS)]
for y_out, sgn in ((-W / 2, 1), (W / 2, -1)):
    vent = (cq.Workplane("XZ", origin=(0, y_out - sgn * 1.0, 0))
            .pushPoints([(x, SLOT_ZC) for x in xs])
            .rect(SLOT_W, SLOT_LEN).extrude(-sgn * (max(T_WALL, T_FRONT) + 1.3))
            .edges("|Y").fillet(SLOT_R))
    body = body.cut(vent)

# ---------------- inner vertical channels behind the front-wall vents ----------------
for x in xs:
    body = body.cut(box(x - CH_W / 2, x + CH_W / 2, -W / 2 + T_FRONT - CH_D, -W / 2 + T_FRONT + 0.05,
                        T_FLOOR, H - CH_TOP))

# ---------------- notch in the front wall ----------------
body = body.cut(box(NOTCH_X0, NOTCH_X1, -W / 2 - 1, -W / 2 + T_FRONT + 0.01, H - NOTCH_DEPTH, H + 1))


# ---------------- clip tabs near the left wall ----------------
def clip_tab(x0, x1, y0, y1, ztop, flare_lo, flare_hi, fh=3.0):
    """thin plate y0..y1, x0..x1 with concave flares on the -Y (lo) / +Y (hi) sides"""
    zf = T_FLOOR
    wp = cq.Workplane("YZ", origin=(x0, 0, 0))
    if flare_lo > 0:
        wp = wp.moveTo(y0 - flare_lo, zf)
    else:
        wp = wp.moveTo(y0, zf - 0.05)
    if flare_hi > 0:
        wp = wp.lineTo(y1 + flare_hi, zf)
        cy, cz = y1 + flare_hi, zf + fh
        wp = wp.threePointArc((cy - flare_hi * math.cos(math.pi / 4), cz - fh * math.sin(math.pi / 4)),
                              (y1, zf + fh))
    else:
        wp = wp.lineTo(y1, zf - 0.05)
    wp = wp.lineTo(y1, ztop).lineTo(y0, ztop)
    if flare_lo > 0:
        wp = wp.lineTo(y0, zf + fh)
        cy, cz = y0 - flare_lo, zf + fh
        wp = wp.threePointArc((cy + flare_lo * math.cos(math.pi / 4), cz - fh * math.sin(math.pi / 4)),
                              (y0 - flare_lo, zf))
    wp = wp.close()
    return wp.extrude(x1 - x0)


TAB_X0, TAB_X1 = -47.4, -44.0
# tab 1: free standing snap clip, thin web with flares both sides and a grooved head
T1_Y0, T1_Y1, T1_TOP, T1_HEAD = 12.2, 12.8, 5.8, 1.3
tab1 = clip_tab(TAB_X0, TAB_X1, T1_Y0, T1_Y1, T1_TOP, 2.5, 2.5, T1_TOP - T1_HEAD - T_FLOOR)
tab1 = tab1.union(box(TAB_X0, TAB_X1, T1_Y0 - 0.25, T1_Y1 + 0.35, T1_TOP - T1_HEAD, T1_TOP))
tab1 = tab1.cut(box(TAB_X0 - 0.1, TAB_X1 + 0.1, T1_Y0 - 0.35, T1_Y0 - 0.05,
                    T1_TOP - T1_HEAD / 2 - 0.1, T1_TOP - T1_HEAD / 2 + 0.1))
# tab 2: short clip on the back edge of opening A
tab2 = clip_tab(TAB_X0, TAB_X1, 1.9, 2.4, 3.9, 0.0, 2.2, 3.9 - T_FLOOR - 0.1)
# tab 3: tall clip on the front edge of opening A
tab3 = clip_tab(TAB_X0, TAB_X1, -6.7, -6.2, 5.5, 2.6, 0.0, 5.5 - T_FLOOR - 0.1)
body = body.union(tab1).union(tab2).union(tab3)

result = body
